import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections

# ---------------------------------------------------------------------------
# Tapered cap / nose body:
#  * smooth lofted shell-less body, rounded-square at the foot, domed at the top
#  * a keel on the back that is a thin fin at the top and fans out to a flat
#    back face further down, with a small latch tab
#  * a slot cut through the upper back of the body (along X) that leaves a thin
#    central web standing in the middle
#  * a notched locating ring under a shallow recess at the bottom
# All driving dimensions are in "reference units" scaled by U (mm per unit).
# ---------------------------------------------------------------------------
U = 0.25  # mm per reference unit

# overall heights
H_RING = 7.3        # height of the notched ring at the bottom
H_WEB = 233.7       # top of the central web
H_FIN = 237.6       # top back corner of the fin

# body loft sections (super-ellipse outlines):
# (height, half width X, front Y, back Y, front exponent, back exponent)
SECTIONS = [
    (H_RING, 35.0, -31.1, 33.6, 2.7, 3.0),
    (60.0, 29.7, -26.6, 32.0, 2.7, 3.0),
    (117.0, 24.0, -19.9, 29.6, 2.65, 3.0),
    (165.0, 19.3, -13.3, 26.6, 2.6, 3.0),
    (200.0, 15.5, -8.1, 23.0, 2.5, 2.9),
    (217.0, 12.6, -4.3, 20.6, 2.4, 2.7),
    (226.0, 9.2, -0.3, 18.7, 2.3, 2.5),
    (231.0, 2.8, 3.3, 16.2, 2.2, 2.3),
]
N_PTS = 24  # points per section outline (smooth periodic spline)

# slot through the upper back of the body: intersection of two elliptic prisms
# along X, offset in Y, which gives the slot its pointed (creased) bottom
SLOT_YC, SLOT_ZC = 9.8, 182.8
SLOT_A, SLOT_B = 11.27, 68.1
SLOT_OFFSET = 1.5

# central web left standing in the slot
T_WEB = 1.5
WEB_PTS = [(3.9, H_WEB), (17.0, H_WEB), (17.0, 215.0), (3.9, 215.0)]

# back keel: YZ outline, flat back face at Y_KEEL; its half width is K_BASE
# below H_KNEE and tapers linearly to K_TOP at the fin top
Y_KEEL = 33.9
H_KEEL_BOT = 38.7        # lowest point of the keel (its foot is a round arc)
H_KEEL_CORNER = 64.7     # where the arc meets the keel corners
K_BASE, K_TOP, H_KNEE = 9.95, 0.475, 138.9
KEEL_PTS = [
    (10.0, H_WEB), (17.0, H_WEB), (Y_KEEL, H_FIN), (Y_KEEL, H_KEEL_BOT - 2),
    (15.0, H_KEEL_BOT - 2), (10.0, 120.0),
]

# latch tab on the keel back (thin plate, YZ plane)
T_TAB = 1.45
TAB_PTS = [(30.0, 137.0), (41.0, 137.0), (41.0, 77.0), (33.9, 67.5), (30.0, 67.5)]

# bottom ring
RING_INSET = 0.8
RING_WALL = 1.5
RECESS_TOP = 9.0
RING_OVERLAP = 0.6
NOTCHES = [(31.3, -16.6, 5.5), (26.9, 26.5, 3.2)]  # (x, y, width), mirrored in X


def u(v):
    return v * U


def section_pts(h, W, yf, yb, nf, nb, inset=0.0):
    W -= inset
    yf += inset
    yb -= inset
    yc = 0.5 * (yf + yb)
    D = 0.5 * (yb - yf)
    pts = []
    for k in range(N_PTS):
        t = math.pi / 2 + 2 * math.pi * k / N_PTS  # start at the back centre
        c, s = math.cos(t), math.sin(t)
        n = nb if s >= 0 else nf
        x = W * math.copysign(abs(c) ** (2.0 / n), c)
        y = yc + D * math.copysign(abs(s) ** (2.0 / n), s)
        pts.append(cq.Vector(u(x), u(y), u(h)))
    return pts


def section_wire(*a, **k):
    params = [i / N_PTS for i in range(N_PTS + 1)]  # same knots on every section
    edge = cq.Edge.makeSpline(section_pts(*a, **k), periodic=True, parameters=params)
    return cq.Wire.assembleEdges([edge])


def smooth_loft(wires, max_degree=3):
    """Smooth (non-ruled) loft kept at low degree so later booleans stay fast."""
    builder = BRepOffsetAPI_ThruSections(True, False, 1e-6)
    builder.SetMaxDegree(max_degree)
    for w in wires:
        builder.AddWire(w.wrapped)
    builder.CheckCompatibility(False)
    builder.Build()
    return cq.Solid(builder.Shape())


def yz_plate(pts, thickness):
    return (
        cq.Workplane("YZ")
        .polyline([(u(y), u(z)) for y, z in pts])
        .close()
        .extrude(u(thickness) / 2.0, both=True)
    )


# ---------------- main body: smooth loft through the sections ----------------
body = cq.Workplane("XY").add(smooth_loft([section_wire(*s) for s in SECTIONS]))

# ---------------- back keel / fin ----------------------------------------------
keel_side = yz_plate(KEEL_PTS, 2.0 * K_BASE + 2.0)
keel_taper = (
    cq.Workplane("XZ")
    .moveTo(u(-K_BASE), u(H_KEEL_CORNER))
    .threePointArc((0, u(H_KEEL_BOT)), (u(K_BASE), u(H_KEEL_CORNER)))
    .lineTo(u(K_BASE), u(H_KNEE))
    .lineTo(u(K_TOP), u(H_FIN))
    .lineTo(u(K_TOP), u(H_FIN + 5))
    .lineTo(u(-K_TOP), u(H_FIN + 5))
    .lineTo(u(-K_TOP), u(H_FIN))
    .lineTo(u(-K_BASE), u(H_KNEE))
    .close()
    .extrude(u(60), both=True)
)
body = body.union(keel_side.intersect(keel_taper))


# ---------------- slot through X (leaves the central web) --------------------
def slot_cutter(sgn):
    """One half of the slot (x > web or x < -web)."""
    halves = []
    for dy in (-SLOT_OFFSET, SLOT_OFFSET):
        halves.append(
            cq.Workplane("YZ", origin=(sgn * u(T_WEB) / 2.0, 0, 0))
            .center(u(SLOT_YC + dy), u(SLOT_ZC))
            .ellipse(u(SLOT_A), u(SLOT_B))
            .extrude(sgn * u(50))
        )
    return halves[0].intersect(halves[1])


body = body.cut(slot_cutter(1)).cut(slot_cutter(-1))

# ---------------- web top and latch tab ----------------------------------------
body = body.union(yz_plate(WEB_PTS, T_WEB)).union(yz_plate(TAB_PTS, T_TAB))

# ---------------- notched ring at the bottom ---------------------------------
s0 = SECTIONS[0]
RING_TOP = H_RING + RING_OVERLAP  # the ring reaches a little into the body
ring_out = cq.Solid.extrudeLinear(
    cq.Face.makeFromWires(section_wire(0.0, *s0[1:], inset=RING_INSET)), cq.Vector(0, 0, u(RING_TOP))
)
ring_in = cq.Solid.extrudeLinear(
    cq.Face.makeFromWires(section_wire(-1.0, *s0[1:], inset=RING_INSET + RING_WALL)),
    cq.Vector(0, 0, u(RING_TOP + 2.0)),
)
ring = cq.Workplane("XY").add(ring_out).cut(cq.Workplane("XY").add(ring_in))

# notches in the ring: (x, y, width) of the front pair and the back pair
W0, yf0, yb0, nf0, nb0 = s0[1:]
yc0 = 0.5 * (yf0 + yb0)
for nx, ny, nw in NOTCHES:
    for sx in (1, -1):
        px, py = sx * nx, ny
        ang = math.degrees(math.atan2(py - yc0, px))
        notch = (
            cq.Workplane("XY")
            .box(u(12), u(nw), u(H_RING) + 0.5, centered=(True, True, False))
            .rotate((0, 0, 0), (0, 0, 1), ang)
            .translate((u(px), u(py), -0.5))
        )
        ring = ring.cut(notch)

# recess in the underside of the body, inside the ring
recess = cq.Solid.extrudeLinear(
    cq.Face.makeFromWires(section_wire(0.0, *s0[1:], inset=RING_INSET + RING_WALL)),
    cq.Vector(0, 0, u(RECESS_TOP)),
)
body = body.cut(cq.Workplane("XY").add(recess), clean=False)
for piece in ring.solids().vals():
    body = body.union(cq.Workplane("XY").add(piece))

result = body
